import cadquery as cq

# =====================================================================
#  HDMI breakout PCB: HDMI-A receptacle (opening +Y), 22-pin FFC
#  connector (actuator -Y) and a handful of SMD parts on a 4-hole PCB.
# =====================================================================

# ---------------------------------------------------------------- PCB
BW, BD, BT = 25.6, 23.0, 1.6        # board width (X), depth (Y), thickness
BR = 2.6                            # corner radius (concentric with holes)
HOLE_D = 2.6                        # mounting hole dia
HOLE_IN = 2.6                       # hole centre inset from the edges
VIA_D = 0.35

# ---------------------------------------------------------------- HDMI
HX = 7.5                            # half width of the shell
HY0, HY1 = 2.55, 14.2               # back / front face of the shell
HZ0 = BT + 0.75                     # shell bottom (overhanging part)
HZW = BT + 1.9                      # side wall lower edge (chamfer start)
HZT = BT + 6.25                     # shell top
HCH = 1.5                           # bottom chamfer (horizontal)
HR_TOP = 1.0                        # top corner radius
HR_BACK = 1.0                       # top-back bend radius
SH_T = 0.3                          # sheet metal thickness
HPINS = 19
LEG_Y = (6.28, 7.39, 8.56, 9.09, 10.11, 10.74)   # side-wall leg / slot stations
LEG_ZT = BT + 3.51                  # top of side slots / L-leg
WRAP_Y1 = 3.2                       # front end of the corner latch tab

# ---------------------------------------------------------------- FFC
FX = 7.95                           # half width of the housing
FY_BACK = -6.84                     # rear face (contacts)
FY_ACT = -8.37                      # actuator rear edge
FY_FRONT = -10.6                    # housing front face
FY_ACT_FRONT = -12.0                # actuator front edge
FH = 1.96                           # housing height
FWALL = 0.7                         # end wall width
FACT_Z0 = 1.25                      # actuator underside (above board)
ACT_DROP = 0.05                     # actuator top sits just below the housing
FPINS = 22
PITCH = 0.5

ZB = BT                             # board top


def box(x0, x1, y0, y1, z0, z1):
    x0, x1 = min(x0, x1), max(x0, x1)
    y0, y1 = min(y0, y1), max(y0, y1)
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cbox(cx, cy, lx, ly, z0, h):
    return box(cx - lx / 2, cx + lx / 2, cy - ly / 2, cy + ly / 2, z0, z0 + h)


def fuse_all(base, items):
    shp = base.val().fuse(*[i.val() for i in items]).clean()
    return cq.Workplane("XY").add(shp)


def cut_all(base, items):
    return cq.Workplane("XY").add(base.val().cut(*[i.val() for i in items]).clean())


# =====================================================================
#  PCB
# =====================================================================
board = (cq.Workplane("XY").box(BW, BD, BT, centered=(True, True, False))
         .edges("|Z").fillet(BR))

hx, hy = BW / 2 - HOLE_IN, BD / 2 - HOLE_IN
board = (board.faces(">Z").workplane()
         .pushPoints([(hx, hy), (-hx, hy), (hx, -hy), (-hx, -hy)])
         .hole(HOLE_D))

VIAS = [(-8.1, 0.85), (-6.48, 0.85), (2.7, 0.5), (3.98, 0.36), (3.06, -0.92),
        (3.61, -1.84), (5.63, -3.09), (10.09, 2.79), (-7.71, -5.87),
        (-6.37, -5.25), (-5.09, -4.48), (0.99, -4.86), (1.98, -4.86),
        (4.63, -7.64), (3.05, -7.63), (1.43, -7.59), (-0.13, -7.56),
        (-1.82, -7.58), (-3.59, -7.76), (-4.58, -7.60), (-2.34, -9.84),
        (8.91, -0.54), (3.32, 6.10), (0.64, 4.76), (-0.99, 4.72),
        (-2.44, 4.72), (-3.71, 4.75), (-5.10, 5.85), (-7.32, -0.86)]
board = board.faces(">Z").workplane().pushPoints(VIAS).hole(VIA_D)

# slotted holes for the HDMI shell legs
board_cuts = []
for sx in (-1, 1):
    board_cuts.append(cq.Workplane("XY").center(sx * 7.25, 3.6)
                      .slot2D(2.4, 0.95, 90).extrude(BT))
    board_cuts.append(cq.Workplane("XY").center(sx * 7.35, 9.62)
                      .slot2D(1.35, 0.7, 90).extrude(BT))
board = cut_all(board, board_cuts)

# =====================================================================
#  HDMI receptacle
# =====================================================================
def hdmi_profile(half_w, z0, zw, zt, ch):
    return [(-half_w, zw), (-half_w, zt), (half_w, zt), (half_w, zw),
            (half_w - ch, z0), (-half_w + ch, z0)]


shell = (cq.Workplane("XZ", origin=(0, HY0, 0))
         .polyline(hdmi_profile(HX, HZ0, HZW, HZT, HCH)).close()
         .extrude(-(HY1 - HY0)))
shell = shell.edges("|Y").edges(">Z").fillet(HR_TOP)
# the back cover is bent down from the top plate (rounded) between the
# corner hooks; the side walls keep square back corners
bend = (box(-5.6, 5.6, HY0 - 0.1, HY0 + HR_BACK, HZT - HR_BACK, HZT + 0.1)
        .cut(cq.Workplane("YZ", origin=(-5.7, 0, 0))
             .center(HY0 + HR_BACK, HZT - HR_BACK).circle(HR_BACK).extrude(11.4)))
shell = shell.cut(bend)
# shallow recess on the back of each corner column (sheet-metal "C" look)
for sx in (-1, 1):
    rec = (cq.Workplane("XZ", origin=(0, HY0 + 0.25, 0))
           .polyline([(sx * 5.75, HZW + 0.3), (sx * 7.0, HZW + 0.3),
                      (sx * 7.0, HZT - 0.5), (sx * 5.75, HZT - 0.5)]).close()
           .extrude(0.5))
    rec = rec.edges("|Y").edges(">Z").edges(">X" if sx > 0 else "<X").fillet(0.5)
    shell = shell.cut(rec)

# ---- additive features that become part of the shell / insulator
adds = []
# lower back insulator + rear legs
adds.append(box(-7.1, 7.1, HY0 + 0.06, HY0 + 2.0, ZB, ZB + 2.0))
for sx in (-1, 1):
    xo = sx * HX
    xi = xo - sx * SH_T
    # rear SMT legs (block + foot) at the back corners
    rleg = box(sx * 5.6, sx * 7.05, 1.95, HY0 + 0.05, ZB, ZB + 2.8)
    rleg = rleg.cut(box(sx * 6.05, sx * 6.6, 1.9, 2.2, ZB - 0.1, ZB + 0.35))
    adds.append(rleg)
    # side walls continued down to the board
    adds.append(box(xo, xi, HY0, LEG_Y[3], ZB, HZW + 0.05))       # rear panel + L-leg foot
    adds.append(box(xo, xi, LEG_Y[4], 11.6, ZB, HZW + 0.05))      # front leg plate
    # latch tab wrapping round the rear corner (back face -> side wall)
    t, xr = 0.3, xo + sx * 0.3
    wrap = (cq.Workplane("XY", origin=(0, 0, ZB + 2.85))
            .polyline([(sx * 5.25, HY0 + 0.05), (sx * 5.25, HY0 - t), (xr, HY0 - t),
                       (xr, WRAP_Y1), (xo - sx * 0.05, WRAP_Y1),
                       (xo - sx * 0.05, HY0 + 0.05)]).close()
            .extrude(1.1))
    wrap = wrap.edges("|Z").edges(cq.selectors.NearestToPointSelector(
        (xr, HY0 - t, ZB + 3.4))).fillet(0.45)
    wrap = wrap.faces("<X" if sx > 0 else ">X").edges("|Y").fillet(0.45)
    adds.append(wrap)
    # rounded hook tabs pressed out of the side wall near the back
    hook = box(xo - sx * 0.05, xo + sx * 0.25, HY0 - 0.05, 4.85, ZB + 3.85, ZB + 4.52)
    adds.append(hook.faces(">Y").edges("|X").fillet(0.3))
    hook = box(xo - sx * 0.05, xo + sx * 0.25, 1.95, 3.5, ZB + 2.3, ZB + 2.85)
    adds.append(hook.faces(">Y").edges("|X").fillet(0.25))
    adds.append(box(sx * 7.0, xo + sx * 0.25, 1.95, HY0 + 0.05, ZB + 2.3, ZB + 2.85))
    # through-board pins
    adds.append(box(sx * 7.0, sx * 7.5, 2.6, 4.6, -0.47, ZB + 0.05))
    adds.append(box(sx * 7.2, sx * 7.5, LEG_Y[3], LEG_Y[4], -0.23, HZW + 0.1))
# SMT contact pins behind the connector
for i in range(HPINS):
    x = -(HPINS - 1) * PITCH / 2 + i * PITCH
    adds.append(box(x - 0.12, x + 0.12, 1.9, HY0 + 0.2, ZB, ZB + 0.18))
    adds.append(box(x - 0.12, x + 0.12, HY0 - 0.2, HY0 + 0.2, ZB, ZB + 0.45))
shell = fuse_all(shell, adds)

# ---- cuts
cuts = []
# receptacle cavity (HDMI-A opening)
cav_depth = HY1 - HY0 - 3.0
cav = (cq.Workplane("XZ", origin=(0, HY1 + 0.01, 0))
       .polyline(hdmi_profile(HX - SH_T, HZ0 + SH_T, HZW + 0.1, HZT - SH_T,
                              HCH - 0.1)).close()
       .extrude(cav_depth))
cav = cav.edges("|Y").edges(">Z").fillet(HR_TOP - SH_T)
cuts.append(cav)
# pressed slot in the back face near the top
cuts.append(cq.Workplane("XZ", origin=(0, HY0 + 0.45, 0))
            .center(0, HZT - 0.75).slot2D(5.4, 1.1, 0).extrude(1.0))
for sx in (-1, 1):
    xo = sx * HX
    # top latch windows
    cuts.append(box(sx * 3.75, sx * 6.08, 7.24, 11.75, HZT - 1.0, HZT + 0.1))
    # lanced opening for the small pressed-down bridges
    cuts.append(box(sx * 1.35, sx * 3.2, 6.0, 7.35, HZT - 1.0, HZT + 0.1))
    # notches in the top-back bend
    cuts.append(box(sx * 3.9, sx * 5.6, HY0 - 0.1, HY0 + 0.9, HZT - 1.5, HZT - 0.42))
    # vertical seam between side wall and back cover
    cuts.append(box(sx * 5.45, sx * 5.7, HY0 - 0.1, HY0 + 0.3, HZW + 0.2, HZT - 1.45))
    # see-through slots either side of the front (through-hole) leg
    for (ya, yb) in ((LEG_Y[2], LEG_Y[3]), (LEG_Y[4] + 0.08, LEG_Y[5])):
        cuts.append(box(xo + sx * 0.1, xo - sx * 0.5, ya, yb, HZW + 0.02, LEG_ZT))
    # thin slits outlining the rear L-shaped leg
    sl = 0.08
    cuts.append(box(xo + sx * 0.1, xo - sx * 0.1, LEG_Y[0] - sl / 2, LEG_Y[0] + sl / 2,
                    ZB + 0.2, LEG_ZT))
    cuts.append(box(xo + sx * 0.1, xo - sx * 0.1, LEG_Y[0], LEG_Y[1], LEG_ZT - sl,
                    LEG_ZT))
    cuts.append(box(xo + sx * 0.1, xo - sx * 0.1, LEG_Y[1] - sl / 2, LEG_Y[1] + sl / 2,
                    HZW, LEG_ZT))
    cuts.append(box(xo + sx * 0.1, xo - sx * 0.1, LEG_Y[1], LEG_Y[3], HZW,
                    HZW + sl))
    cuts.append(box(xo + sx * 0.1, xo - sx * 0.1, LEG_Y[4] - sl / 2, LEG_Y[4] + sl / 2,
                    HZW, LEG_ZT))
shell = cut_all(shell, cuts)

# ---- parts living inside the cavity / windows
inner = []
inner.append(box(-5.0, 5.0, HY1 - cav_depth - 0.1, HY1 - 1.6, ZB + 3.6, ZB + 4.5))
for sx in (-1, 1):
    spring = box(sx * 1.9, sx * 2.85, HY1 - 4.4, HY1 - 2.2,
                 HZ0 + SH_T - 0.05, HZ0 + SH_T + 0.15)
    inner.append(spring.rotate((0, HY1 - 4.4, HZ0 + SH_T),
                               (1, HY1 - 4.4, HZ0 + SH_T), 10))
    # latch spring: hinged at the back edge of the window, dipping forwards
    # with a sharply bent tip
    lx0, lx1 = sx * 3.85, sx * 5.4
    tl = 4.25                                   # tongue length from hinge
    tongue = box(lx0, lx1, 7.0, 7.24 + tl, HZT - SH_T, HZT)
    inner.append(tongue.rotate((0, 7.24, HZT), (1, 7.24, HZT), -7))
    ty, tz = 7.24 + tl * 0.9925, HZT - tl * 0.1219
    tip = box(lx0, lx1, ty - 0.06, ty + 0.4, tz - SH_T, tz)
    inner.append(tip.rotate((0, ty, tz), (1, ty, tz), -30))
    # pressed bridge between two lanced slits (reads as "II" from above)
    bt, dp = 0.2, 0.35
    prof = [(1.28, HZT), (1.74, HZT - dp), (2.93, HZT - dp), (3.27, HZT),
            (3.27, HZT - bt), (2.97, HZT - dp - bt), (1.70, HZT - dp - bt),
            (1.28, HZT - bt)]
    prof = [(sx * px, pz) for (px, pz) in prof]
    bridge = (cq.Workplane("XZ", origin=(0, 6.06, 0)).polyline(prof).close()
              .extrude(-(7.29 - 6.06)))
    inner.append(bridge)
hdmi = fuse_all(shell, inner)

# =====================================================================
#  FFC connector
# =====================================================================
ffc = box(-FX, FX, FY_ACT, FY_BACK, ZB, ZB + FH)                 # rear body
f_adds = []
for sx in (-1, 1):
    f_adds.append(box(sx * FX, sx * (FX - FWALL), FY_FRONT, FY_ACT + 0.05, ZB, ZB + FH))
f_adds.append(box(-FX + FWALL - 0.05, FX - FWALL + 0.05, FY_FRONT, FY_ACT + 0.05,
                  ZB, ZB + FACT_Z0))
# actuator
act = box(-7.25, 7.25, FY_ACT_FRONT, FY_ACT, ZB + FACT_Z0, ZB + FH - ACT_DROP)
act = act.faces("<Y").edges("<Z").chamfer(0.3)
f_adds.append(act)
# lugs at both ends of the actuator reaching down towards the board
for sx in (-1, 1):
    lug = box(sx * 6.55, sx * 7.25, FY_ACT_FRONT, FY_FRONT + 0.05, ZB + 0.45,
              ZB + FH - ACT_DROP)
    lug = lug.cut(box(sx * 7.0, sx * 7.3, FY_ACT_FRONT - 0.1, FY_FRONT,
                      ZB + 0.4, ZB + 0.9))
    f_adds.append(lug)
# small posts at the rear corners of the housing
for sx in (-1, 1):
    f_adds.append(box(sx * (FX - 0.5), sx * FX, FY_BACK, FY_BACK - 0.3, ZB,
                      ZB + FH + 0.08))
# contact feet at the back
for i in range(FPINS):
    x = -(FPINS - 1) * PITCH / 2 + i * PITCH
    f_adds.append(box(x - 0.12, x + 0.12, FY_BACK - 0.1, FY_BACK + 0.3, ZB, ZB + 0.15))
ffc = fuse_all(ffc, f_adds)

f_cuts = []
for sx in (-1, 1):
    # pockets at the rear corners of the actuator
    f_cuts.append(box(sx * 5.7, sx * 7.26, FY_ACT - 0.75, FY_ACT + 0.01,
                      ZB + FH - 0.5, ZB + FH + 0.1))
    # recessed windows on the end faces
    f_cuts.append(box(sx * (FX + 0.05), sx * (FX - 0.15), -9.9, -7.1,
                      ZB + 0.35, ZB + 1.6))
# contact comb on the rear face
for i in range(FPINS):
    x = -(FPINS - 1) * PITCH / 2 + i * PITCH
    f_cuts.append(box(x - 0.1, x + 0.1, FY_BACK - 0.01, FY_BACK - 0.55,
                      ZB + 0.2, ZB + FH - 0.35))
ffc = cut_all(ffc, f_cuts)


# =====================================================================
#  SMD parts
# =====================================================================
def chip(cx, cy, length, width, h, along_y=True, cap=0.3):
    lx, ly = (width, length) if along_y else (length, width)
    items = [cbox(cx, cy, lx, ly, ZB, h)]
    for s in (-1, 1):
        if along_y:
            items.append(cbox(cx, cy + s * (length / 2 - cap / 2), width + 0.04,
                              cap, ZB, h + 0.03))
        else:
            items.append(cbox(cx + s * (length / 2 - cap / 2), cy, cap,
                              width + 0.04, ZB, h + 0.03))
    return items


def array(cx, cy, along_y=True):
    length, width, h = 3.15, 1.65, 0.45
    lx, ly = (width, length) if along_y else (length, width)
    items = [cbox(cx, cy, lx, ly, ZB, h)]
    for s in (-1, 1):
        for k in range(4):
            t = -1.2 + k * 0.8
            if along_y:
                items.append(cbox(cx + s * (width / 2 - 0.15), cy + t,
                                  0.34, 0.45, ZB, h + 0.05))
            else:
                items.append(cbox(cx + t, cy + s * (width / 2 - 0.15),
                                  0.45, 0.34, ZB, h + 0.05))
    return items


def gull_lead(length, zh, w, t=0.12):
    """gull-wing lead pointing +X, root at x=0, foot on the board"""
    a, b = 0.12, 0.32
    pts = [(-0.08, zh), (a, zh), (b, 0.0), (length, 0.0), (length, t),
           (b + 0.04, t), (a + 0.04, zh + t), (-0.08, zh + t)]
    return (cq.Workplane("XZ").polyline(pts).close()
            .extrude(w / 2, both=True))


def sot(cx, cy, bl, bw, h, pitch, span, leads_along_x=True, lw=0.38):
    # bl: body length along the lead rows, bw: body width across them
    if leads_along_x:
        body = cbox(cx, cy, bw, bl, ZB + 0.1, h - 0.1)
    else:
        body = cbox(cx, cy, bl, bw, ZB + 0.1, h - 0.1)
    body = body.edges(">Z").chamfer(0.08)
    items = [body]
    zh = (h - 0.1) * 0.45
    for s in (-1, 1):
        for k in (-1, 0, 1):
            lead = gull_lead(span / 2 - bw / 2, zh, lw)
            if leads_along_x:
                ang = 0 if s > 0 else 180
                lead = (lead.rotate((0, 0, 0), (0, 0, 1), ang)
                        .translate((cx + s * bw / 2, cy + k * pitch, ZB)))
            else:
                ang = 90 if s > 0 else -90
                lead = (lead.rotate((0, 0, 0), (0, 0, 1), ang)
                        .translate((cx + k * pitch, cy + s * bw / 2, ZB)))
            items.append(lead)
    return items


parts = []
parts += chip(-11.2, 2.65, 1.65, 0.95, 0.8)          # 0603 resistors
parts += chip(-9.04, 2.9, 1.65, 0.95, 0.8)
parts += chip(9.19, 4.76, 1.65, 0.95, 0.8)
parts += chip(11.0, 4.86, 1.65, 0.95, 0.8)
parts += chip(11.76, -1.1, 1.65, 0.95, 0.8)
parts += chip(5.65, -0.81, 2.05, 1.33, 1.0)          # 0805 capacitors
parts += chip(10.08, 1.5, 2.05, 1.33, 1.0, along_y=False)
parts += array(-10.08, -0.92, along_y=True)          # 4x resistor arrays
parts += array(-3.55, -0.79, along_y=False)
parts += array(0.55, -0.80, along_y=False)
parts += sot(8.97, -1.24, 2.9, 1.6, 1.1, 0.95, 2.9, leads_along_x=True)   # SOT-23-6
parts += sot(-7.26, -0.92, 2.0, 1.2, 0.95, 0.65, 2.2, leads_along_x=False,
             lw=0.3)                                                          # SC-70-6

result = fuse_all(board, [hdmi, ffc] + parts)
